import math
import cadquery as cq

# =====================================================================
# Bent sheet bracket: flat "H"-frame plate (XZ plane, thickness +Y) with
# two open-end jaws on the left and a right bar whose two ends are bent
# back (+Y) into inclined eyes carrying cylindrical bosses along Y.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------------------
T = 2.4                 # sheet thickness
JAW_R = 6.85            # radius of the open-end jaw cut-outs
TAB_R = 5.75            # radius of the round eyes / bosses
HOLE_R = 2.75           # through hole in eyes and bosses (axis along Y)
BOSS_END_Y = 32.4       # Y of the flat end faces of the bosses
SPLIT_X = 2.0           # only material right of this X is bent
BOSS_EPS = 0.05         # boss cylinder oversize, trimmed back by the eye outline
FLARE_Y = 24.0          # Y where the boss starts to flare towards the strip
FLARE_R = 24.0          # radius of the concave flare arc of the boss

TOP_JAW_C = (-14.28, 47.02)
BOT_JAW_C = (-21.57, -40.80)
TOP_TAB_C = (19.43, 53.85)
BOT_TAB_C = (9.93, -53.58)

TOP_JAW_TIPS = (125.0, 35.7)     # deg, jaw tip positions on the jaw circle
BOT_JAW_TIPS = (227.7, 311.0)
TOP_TAB_ANG = (26.0, 205.0)      # deg, where the bar edges meet the eye
BOT_TAB_ANG = (148.0, 5.0)

# bend lines (perpendicular to the bar, i.e. tilted in the XZ plane)
TOP_BEND_ORIGIN = (19.43, 33.4)  # point of the upper bend line (X, Z)
TOP_BEND_TILT = 12.0             # deg, bend axis rises to +X
BOT_BEND_ORIGIN = (9.93, -33.5)
BOT_BEND_TILT = 6.0              # deg, bend axis falls to +X

# side profile of the bent end (outer / convex surface) in local coords
#   u = Y (depth), v = distance from the bend line along the bar:
#   bend arc R1 (vertical -> RUN_ANG), straight run, end arc END_R that
#   levels out on top of the boss at the boss end plane
RUN_ANG = 30.0                   # deg, inclination of the straight run
END_R = 6.0                      # outer radius of the end rounding arc
ARM_END_V = 25.7                 # v of the eye top above the bend line


def pol(c, r, a):
    a = math.radians(a)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


# ---------------- front outline (XZ) ---------------------------------
left_side = [
    (-20.7, 51.35), (-22.45, 48.9), (-23.25, 46.25), (-22.9, 43.6),
    (-21.6, 41.4), (-19.35, 38.75), (-16.3, 35.0), (-12.3, 28.0),
    (-9.3, 20.0), (-7.9, 12.0), (-7.8, 4.0), (-9.0, -4.0), (-11.6, -12.0),
    (-14.3, -18.0), (-17.0, -22.5), (-20.1, -26.6), (-24.1, -30.6),
    (-28.3, -34.3), (-30.0, -38.0), (-29.75, -41.6), (-28.4, -44.4),
]
lower_gap = [
    (-14.55, -44.85), (-13.15, -42.55), (-12.45, -39.75), (-12.2, -36.85),
    (-11.7, -34.15), (-9.55, -31.45), (-6.3, -29.3), (-2.55, -28.65),
    (2.3, -28.75), (5.55, -29.85), (7.7, -32.0), (9.05, -35.25),
    (9.6, -39.0), (9.05, -42.75), (7.7, -46.0),
]
right_outer = [
    (15.45, -49.0), (15.2, -45.0), (15.1, -41.3), (15.3, -34.4),
    (15.9, -28.35), (16.75, -22.3), (18.05, -16.25), (20.0, -10.1),
    (22.7, -3.05), (25.3, 3.85), (27.65, 10.8), (29.2, 17.7),
    (30.05, 24.6), (30.25, 29.8), (30.05, 35.0), (29.05, 43.25),
    (28.0, 47.0),
]
upper_gap = [
    (16.95, 48.25), (18.5, 44.55), (19.3, 40.35), (19.05, 36.65),
    (17.45, 32.9), (14.8, 30.3), (11.1, 28.7), (6.85, 28.45),
    (2.0, 28.8), (-1.05, 30.3), (-4.25, 33.45), (-6.1, 37.15),
    (-6.45, 40.85), (-6.1, 44.05), (-6.6, 47.2),
]
window_pts = [
    (-2.2, 19.15), (-0.6, 21.4), (1.6, 22.0), (10.6, 22.1), (17.45, 23.55),
    (20.6, 23.8), (22.6, 22.3), (23.1, 19.3), (21.35, 10.3), (16.0, -3.4),
    (12.05, -14.15), (10.9, -19.5), (9.6, -22.0), (7.6, -22.7), (3.0, -22.1),
    (-4.1, -22.0), (-6.1, -20.5), (-6.5, -17.4), (-5.55, -14.15),
    (-2.45, -4.35), (-1.3, 5.3), (-1.9, 13.35),
]

tj_l = pol(TOP_JAW_C, JAW_R, TOP_JAW_TIPS[0])
tj_r = pol(TOP_JAW_C, JAW_R, TOP_JAW_TIPS[1])
bj_l = pol(BOT_JAW_C, JAW_R, BOT_JAW_TIPS[0])
bj_r = pol(BOT_JAW_C, JAW_R, BOT_JAW_TIPS[1])
bt_a = pol(BOT_TAB_C, TAB_R, BOT_TAB_ANG[0])
bt_b = pol(BOT_TAB_C, TAB_R, BOT_TAB_ANG[1])
tt_a = pol(TOP_TAB_C, TAB_R, TOP_TAB_ANG[0])
tt_b = pol(TOP_TAB_C, TAB_R, TOP_TAB_ANG[1])


def tan_ccw(a):
    a = math.radians(a)
    return (-math.sin(a), math.cos(a))


def tlist(pts, t_start, t_end):
    """tangent list for spline(..., includeCurrent=True): only ends set"""
    n = len(pts) + 1
    return [t_start] + [None] * (n - 2) + [t_end]


def spl(w, pts, t_start=None, t_end=None):
    """spline from the current point through pts with optional end tangents
    (unit tangents, chord-length parametrisation)"""
    if t_start is None and t_end is None:
        return w.spline(pts, includeCurrent=True)
    return w.spline(pts, includeCurrent=True, scale=False,
                    tangents=tlist(pts, t_start, t_end))


def outline(wp):
    w = wp.moveTo(*tj_l)
    w = spl(w, left_side + [bj_l])
    w = w.threePointArc(pol(BOT_JAW_C, JAW_R, 90.0), bj_r)
    w = spl(w, lower_gap + [bt_a], None, tan_ccw(BOT_TAB_ANG[0]))
    mid = 0.5 * (BOT_TAB_ANG[0] + BOT_TAB_ANG[1] + 360.0)
    w = w.threePointArc(pol(BOT_TAB_C, TAB_R, mid), bt_b)
    w = spl(w, right_outer + [tt_a], tan_ccw(BOT_TAB_ANG[1]),
            tan_ccw(TOP_TAB_ANG[0]))
    mid = 0.5 * (TOP_TAB_ANG[0] + TOP_TAB_ANG[1])
    w = w.threePointArc(pol(TOP_TAB_C, TAB_R, mid), tt_b)
    w = spl(w, upper_gap + [tj_r], tan_ccw(TOP_TAB_ANG[1]), None)
    mid = 0.5 * (TOP_JAW_TIPS[0] + TOP_JAW_TIPS[1]) + 180.0
    w = w.threePointArc(pol(TOP_JAW_C, JAW_R, mid), tj_l)
    return w.close()


BIG = 200.0

front_prism = outline(cq.Workplane("XZ", origin=(0, BIG / 2, 0))).extrude(BIG)
window_prism = (cq.Workplane("XZ", origin=(0, BIG / 2, 0))
                .spline(window_pts, periodic=True).close().extrude(BIG))
front_prism = front_prism.cut(window_prism)


# ---------------- bend frames -----------------------------------------
def bend_plane(origin, tilt, sign, shift=0.0):
    """plane: local x = +Y, local y = along the bar away from the bend
    line (towards the eye), normal = bend axis.  'shift' moves the plane
    along its normal (used to extrude symmetric prisms without a seam)."""
    t = math.radians(tilt)
    axis = cq.Vector(math.cos(t), 0.0, sign * math.sin(t)) * sign
    return cq.Plane(origin=cq.Vector(origin[0], 0.0, origin[1]) + axis * shift,
                    xDir=cq.Vector(0, 1, 0), normal=axis)


def zone(origin, tilt, sign):
    """half space beyond the bend line, restricted to X > SPLIT_X"""
    pl = bend_plane(origin, tilt, sign, -BIG)
    half = (cq.Workplane(pl).center(0, BIG / 2).rect(2 * BIG, BIG)
            .extrude(2 * BIG))
    right = (cq.Workplane("XY").box(BIG, BIG, 3 * BIG, centered=(False, True, True))
             .translate((SPLIT_X, 0, 0)))
    return half.intersect(right)


def arm_geometry():
    """solve the bend radius and run length so the profile ends at
    (BOSS_END_Y, ARM_END_V) with a horizontal tangent"""
    b = math.radians(RUN_ANG)
    sb, cb = math.sin(b), math.cos(b)
    du = BOSS_END_Y - END_R * sb
    dv = ARM_END_V - END_R * (1 - cb)
    # du = R1 (1 - sb) + L cb ; dv = R1 cb + L sb
    det = (1 - sb) * sb - cb * cb
    r1 = (du * sb - dv * cb) / det
    run = (dv * (1 - sb) - du * cb) / det
    return r1, run


R1, RUN = arm_geometry()


def arm_points(off, n_arc=5, n_run=4, n_end=3):
    """sample points of the side profile (bend arc R1 -> straight run ->
    end arc END_R), offset by 'off' towards the concave side"""
    b = math.radians(RUN_ANG)
    sb, cb = math.sin(b), math.cos(b)
    r = R1 - off
    t1 = math.radians(90.0 - RUN_ANG)
    pts = [(R1 - r * math.cos(t1 * k / n_arc), r * math.sin(t1 * k / n_arc))
           for k in range(n_arc + 1)]
    q1 = (R1 - R1 * sb, R1 * cb)                      # outer arc end
    q2 = (q1[0] + RUN * cb, q1[1] + RUN * sb)         # outer run end
    c2 = (q2[0] + END_R * sb, q2[1] - END_R * cb)     # end arc centre
    r2 = END_R - off
    p1 = pts[-1]
    p2 = (c2[0] - r2 * sb, c2[1] + r2 * cb)
    pts += [(p1[0] + (p2[0] - p1[0]) * k / n_run, p1[1] + (p2[1] - p1[1]) * k / n_run)
            for k in range(1, n_run + 1)]
    pts += [(c2[0] - r2 * math.sin(b * (1 - k / n_end)),
             c2[1] + r2 * math.cos(b * (1 - k / n_end))) for k in range(1, n_end + 1)]
    return pts


def profile_spline(w, pts, reverse=False):
    """smooth spline through the profile points (vertical start tangent,
    horizontal end tangent)"""
    t0, t1 = (0.0, 1.0), (1.0, 0.0)
    if reverse:
        pts = list(reversed(pts))
        t0, t1 = (-1.0, 0.0), (0.0, -1.0)
    tl = [t0] + [None] * (len(pts) - 2) + [t1]
    return w.spline(pts[1:], includeCurrent=True, tangents=tl, scale=False)


def strip_solid(origin, tilt, sign):
    pl = bend_plane(origin, tilt, sign, -BIG)
    outer = arm_points(0.0)
    inner = arm_points(T)
    w = cq.Workplane(pl).moveTo(0.0, -2.0).lineTo(*outer[0])
    w = profile_spline(w, outer).lineTo(*inner[-1])
    w = profile_spline(w, inner, reverse=True)
    return w.lineTo(T, -2.0).close().extrude(2 * BIG)


def concave_region(origin, tilt, sign, off):
    """region on the concave side of the strip (offset 'off' inside the
    sheet), up to the boss end plane"""
    pl = bend_plane(origin, tilt, sign, -BIG)
    mid = arm_points(off)
    w = profile_spline(cq.Workplane(pl).moveTo(*mid[0]), mid)
    return (w.lineTo(BOSS_END_Y, -10.0).lineTo(mid[0][0], -10.0).close()
            .extrude(2 * BIG))


def trumpet(c):
    """boss behind the eye: cylinder of the eye radius at the far end that
    flares out (concave quarter arc of radius FLARE_R) towards the sheet -
    a solid of revolution about the hole axis (parallel to Y)"""
    r0 = TAB_R + BOSS_EPS
    y0 = max(FLARE_Y - FLARE_R, 0.5 * T)
    cy, cr = FLARE_Y, r0 + FLARE_R                  # flare arc centre (Y, r)

    def on_arc(y):
        return (y, cr - math.sqrt(max(FLARE_R ** 2 - (cy - y) ** 2, 0.0)))

    p_start = on_arc(y0)
    p_mid = on_arc(0.5 * (y0 + FLARE_Y))
    pl = cq.Plane(origin=cq.Vector(c[0], 0.0, c[1]),
                  xDir=cq.Vector(0, 1, 0), normal=cq.Vector(1, 0, 0))
    return (cq.Workplane(pl)
            .moveTo(y0, 0.0).lineTo(*p_start)
            .threePointArc(p_mid, (FLARE_Y, r0))
            .lineTo(BOSS_END_Y, r0).lineTo(BOSS_END_Y, 0.0).close()
            .revolve(360.0, (0, 0, 0), (1, 0, 0)))


def bent_end(c, origin, tilt, sign):
    """bent strip + flared boss behind the eye, clipped to the front
    outline (the eye outline trims the boss exactly)"""
    boss = trumpet(c).intersect(concave_region(origin, tilt, sign, 0.5 * T))
    body = strip_solid(origin, tilt, sign).union(boss)
    return body.intersect(zone(origin, tilt, sign)).intersect(front_prism)


# ---------------- assemble --------------------------------------------
top_end = bent_end(TOP_TAB_C, TOP_BEND_ORIGIN, TOP_BEND_TILT, +1)
bot_end = bent_end(BOT_TAB_C, BOT_BEND_ORIGIN, BOT_BEND_TILT, -1)

slab = cq.Workplane("XY").box(BIG, T, BIG, centered=(True, False, True))
plate = (front_prism.intersect(slab)
         .cut(zone(TOP_BEND_ORIGIN, TOP_BEND_TILT, +1))
         .cut(zone(BOT_BEND_ORIGIN, BOT_BEND_TILT, -1)))

result = plate.union(top_end).union(bot_end)

for c in (TOP_TAB_C, BOT_TAB_C):
    hole = (cq.Workplane("XZ", origin=(0, BIG / 2, 0))
            .center(c[0], c[1]).circle(HOLE_R).extrude(BIG))
    result = result.cut(hole)

VIEW = {"azimuth": 45, "elevation": 26}
